import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
TUBE_R = 20.0          # main tube outer radius
TUBE_L = 73.0          # main tube length (along Y)
BORE_R = 15.8          # main tube bore radius
BORE_CH_R = 2.0        # bore-mouth chamfer, radial size (both ends)
BORE_CH_ANG = 55.0     # chamfer half-angle from the bore axis

LOBE_R = 12.5          # side lobe outer radius
LOBE_DIST = 33.0       # axis-to-axis distance tube -> lobe (along +X)
LOBE_L = 54.6          # lobe length, flush with the tube front face (y = 0)
LOBE_BORE_R = 10.0     # blind bore in the lobe, from its back end
LOBE_BORE_D = 40.0     # depth of that blind bore

NECK_R = 5.0           # concave blend radius between tube and lobe
NECK_CREASE = 0.0      # deg: 0 = blend tangent to the tube

# where the (unavoidable) seam lines of the round faces are parked, deg about Y
# measured from +X toward +Z
SEAM_TUBE = 230.0
SEAM_BORE = 45.0
SEAM_LOBE_BORE = 135.0

R, r, d, f = TUBE_R, LOBE_R, LOBE_DIST, NECK_R
BORE_CH_A = BORE_CH_R / math.tan(math.radians(BORE_CH_ANG))   # axial size

# ---------------- blend circle geometry ----------------
# tangent to the lobe (|c-(d,0)| = r+f), crossing the tube circle at NECK_CREASE
th = math.radians(NECK_CREASE)
D = math.sqrt(R * R + f * f + 2.0 * R * f * math.cos(th))   # |c|
xf = (D * D - (r + f) ** 2 + d * d) / (2.0 * d)
yf = math.sqrt(D * D - xf * xf)


def pol(cx, cy, rad, ang):
    return (cx + rad * math.cos(ang), cy + rad * math.sin(ang))


# angles seen from the upper blend centre (xf, yf)
a_org = math.atan2(-yf, -xf)                     # toward tube axis
alpha = math.acos(max(-1.0, min(1.0, (D * D + f * f - R * R) / (2.0 * D * f))))
a_P = a_org + alpha                              # crossing nearer the neck
a_L = math.atan2(-yf, d - xf)                    # toward lobe axis (tangency)
P1 = pol(xf, yf, f, a_P)
L1 = pol(xf, yf, f, a_L)
M1 = pol(xf, yf, f, 0.5 * (a_P + a_L))
P2 = (P1[0], -P1[1])
L2 = (L1[0], -L1[1])
M2 = (M1[0], -M1[1])

Y_AXIS = ((0, 0, 0), (0, 1, 0))

# ---------------- main tube ----------------
# Workplane "XZ": local x = X, local y = Z, extrude(-L) runs toward +Y
tube = (
    cq.Workplane("XZ").circle(R).extrude(-TUBE_L)            # y: 0 .. TUBE_L
    .rotate(*Y_AXIS, -SEAM_TUBE)                             # park the seam
)

# ---------------- lobe + neck (region outside the tube) ----------------
lobe = (
    cq.Workplane("XZ")
    .moveTo(*P1)
    .threePointArc(M1, L1)
    .threePointArc((d + r, 0.0), L2)
    .threePointArc(M2, P2)
    .threePointArc((R, 0.0), P1)
    .close()
    .extrude(-LOBE_L)
)

body = tube.union(lobe)

# ---------------- main bore with chamfered mouths (revolved cutter) ----------------
cr, ca = BORE_CH_R, BORE_CH_A
e = 1.0
bore_profile = [
    (0.0, -e),
    (BORE_R + cr + e, -e),
    (BORE_R + cr + e, 0.0),
    (BORE_R + cr, 0.0),
    (BORE_R, ca),
    (BORE_R, TUBE_L - ca),
    (BORE_R + cr, TUBE_L),
    (BORE_R + cr + e, TUBE_L),
    (BORE_R + cr + e, TUBE_L + e),
    (0.0, TUBE_L + e),
]
bore_cut = (
    cq.Workplane("XY")
    .polyline(bore_profile)
    .close()
    .revolve(360.0, (0, 0, 0), (0, 1, 0))
    .rotate(*Y_AXIS, -SEAM_BORE)
)
body = body.cut(bore_cut)

# ---------------- blind bore in the lobe, from its back end ----------------
lobe_bore = (
    cq.Workplane("XZ", origin=(0, LOBE_L, 0))
    .center(d, 0)
    .circle(LOBE_BORE_R)
    .extrude(LOBE_BORE_D)          # XZ normal is -Y: from the back end toward the front
    .rotate((d, 0, 0), (d, 1, 0), -SEAM_LOBE_BORE)
)
body = body.cut(lobe_bore)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
